import math
import cadquery as cq

# ---------------------------------------------------------------
# Chain-drive module: two thin stadium plates, a double sprocket at
# each end between the plates and a second double sprocket hanging
# below the -X end on a hub.
# ---------------------------------------------------------------

# sprocket tooth form (10 teeth): flat root arcs between convex,
# bullet shaped teeth with a narrow flat top
N_TEETH = 10
PITCH = 12.7
TIP_R = PITCH * (0.6 + 1 / math.tan(math.pi / N_TEETH)) / 2
OD = 2 * TIP_R
ROOT_R = 0.75 * TIP_R             # valley floor radius
BASE_HALF = 10.6                  # tooth half angle at the root (deg)
MID_R = 0.857 * TIP_R             # control point of the flank arc
MID_HALF = 7.9                    # tooth half angle at MID_R (deg)
TIP_HALF = 1.8                    # half angle of the flat tooth top (deg)

# vertical stack (mm)
PLATE_T = 1.15           # side plate thickness
SP_T = 3.76              # single sprocket thickness
SP_GAP = 1.5            # gap between the two sprockets of a pair
PLATE_GAP = 1.65         # gap plate <-> sprocket
COLLAR_H = 1.42
COLLAR_D = 17.6
NECK_H = 3.45
NECK_D = 14.0
NUT_H = 4.65
NUT_D = 17.6

# plan
CENTER_DIST = 79.4      # sprocket centre distance
PLATE_W = 35.4          # plate width (ends are semicircles)
YAW = -4.5              # whole module is turned about Z

HUB_D_TOP = 12.6        # round spacer plate -> sprocket
HUB_AF_MID = 12.4       # hex spacer between sprockets (across flats)
HUB_D_BEAR = 17.2       # bearing flange above the lower plate (drive end)

PLATE_HOLE_D = 1.2
PLATE_HOLE_SQ = 3.1     # square pattern of small holes round each axle

BORE_D = 9.0            # round bore of the lower drive stack
HEX_AF = 11.9           # hex recess across flats on the bottom face
HEX_DEPTH = 0.6
HEX_RELIEF_D = 1.0      # corner reliefs of the hex pocket
BOLT_CIRCLE_D = 23.4
BOLT_HOLE_D = 2.2
N_BOLT = 6
PIN_CIRCLE_D = 15.0
PIN_HOLE_D = 1.0


def _pol(r, a):
    return (r * math.cos(a), r * math.sin(a))


def sprocket_blank(thk, phase=0.0):
    """Closed 10 tooth outline built from arcs, extruded to thk."""
    step = 2 * math.pi / N_TEETH
    b = math.radians(BASE_HALF)
    m = math.radians(MID_HALF)
    t = math.radians(TIP_HALF)
    wp = cq.Workplane("XY").moveTo(*_pol(ROOT_R, phase - b))
    for k in range(N_TEETH):
        a = phase + k * step
        wp = wp.threePointArc(_pol(MID_R, a - m), _pol(TIP_R, a - t))
        wp = wp.threePointArc(_pol(TIP_R, a), _pol(TIP_R, a + t))
        wp = wp.threePointArc(_pol(MID_R, a + m), _pol(ROOT_R, a + b))
        if k < N_TEETH - 1:
            wp = wp.threePointArc(_pol(ROOT_R, a + step / 2),
                                  _pol(ROOT_R, a + step - b))
        else:
            wp = wp.threePointArc(_pol(ROOT_R, a + step / 2),
                                  _pol(ROOT_R, phase - b))
    return wp.close().extrude(thk)


def stadium(length, width, thk):
    return (cq.Workplane("XY").slot2D(length + width, width, 0).extrude(thk))


# ---------------- build -----------------------------------------
# phases of the tooth pattern (degrees, in the world frame)
PHASE_L = 18.0          # drive end (-X): valley on the long axis
PHASE_R = 1.5           # idler end (+X): tooth on the long axis

zB2 = 0.0
zB1 = zB2 + SP_T + SP_GAP
zNut = zB1 + SP_T
zNeck = zNut + NUT_H
zCollar = zNeck + NECK_H
zPlateLow = zCollar + COLLAR_H
zA2 = zPlateLow + PLATE_T + PLATE_GAP
zA1 = zA2 + SP_T + SP_GAP
zPlateTop = zA1 + SP_T + PLATE_GAP

xL = -CENTER_DIST / 2
xR = CENTER_DIST / 2
phL = math.radians(PHASE_L - YAW)
phR = math.radians(PHASE_R - YAW)


def cyl(d, h, x, z0):
    return cq.Workplane("XY").circle(d / 2).extrude(h).translate((x, 0, z0))


def hexp(af, h, x, z0):
    # hex prism, flats facing +-X (corners on the Y axis)
    return (cq.Workplane("XY").polygon(6, af / math.cos(math.pi / 6))
            .extrude(h).rotate((0, 0, 0), (0, 0, 1), 30)
            .translate((x, 0, z0)))


parts = []

# side plates
for zp in (zPlateLow, zPlateTop):
    parts.append(stadium(CENTER_DIST, PLATE_W, PLATE_T).translate((0, 0, zp)))

# double sprockets between the plates
for xc, ph, bear in ((xL, phL, True), (xR, phR, False)):
    parts.append(sprocket_blank(SP_T, ph).translate((xc, 0, zA1)))
    parts.append(sprocket_blank(SP_T, ph).translate((xc, 0, zA2)))
    parts.append(cyl(HUB_D_TOP, PLATE_GAP, xc, zA1 + SP_T))
    parts.append(hexp(HUB_AF_MID, SP_GAP, xc, zA2 + SP_T))
    if bear:
        parts.append(cyl(HUB_D_BEAR, PLATE_GAP, xc, zPlateLow + PLATE_T))
    else:
        parts.append(cyl(HUB_D_TOP, PLATE_GAP, xc, zPlateLow + PLATE_T))

# output stack below the drive end
parts.append(sprocket_blank(SP_T, phL).translate((xL, 0, zB1)))
parts.append(sprocket_blank(SP_T, phL).translate((xL, 0, zB2)))
parts.append(hexp(HUB_AF_MID, SP_GAP, xL, zB2 + SP_T))
parts.append(cyl(NUT_D, NUT_H, xL, zNut))
parts.append(cyl(NECK_D, NECK_H, xL, zNeck))
parts.append(cyl(COLLAR_D, COLLAR_H, xL, zCollar))

body = parts[0]
for p_ in parts[1:]:
    body = body.union(p_)

# small holes round the axles (square pattern turned 45 deg)
def hole_square(xc):
    r = PLATE_HOLE_SQ / math.sqrt(2)
    return [(xc + r * math.cos(a), r * math.sin(a))
            for a in (0, math.pi / 2, math.pi, 1.5 * math.pi)]

top_pts = hole_square(xL) + hole_square(xR)
body = body.cut(cq.Workplane("XY").pushPoints(top_pts).circle(PLATE_HOLE_D / 2)
                .extrude(PLATE_T + 0.2).translate((0, 0, zPlateTop - 0.1)))
body = body.cut(cq.Workplane("XY").pushPoints(hole_square(xR))
                .circle(PLATE_HOLE_D / 2)
                .extrude(PLATE_T + 0.2).translate((0, 0, zPlateLow - 0.1)))

# bore, hex recess, bolt and pin holes in the output stack
body = body.cut(cyl(BORE_D, zPlateLow + 0.1, xL, -0.1))
hex_ac = HEX_AF / math.cos(math.pi / 6)
hex_recess = (cq.Workplane("XY").polygon(6, hex_ac)
              .extrude(HEX_DEPTH + 0.1))
# small round reliefs in the six corners of the hex pocket
reliefs = (cq.Workplane("XY")
           .pushPoints([_pol(hex_ac / 2, i * math.pi / 3) for i in range(6)])
           .circle(HEX_RELIEF_D / 2).extrude(HEX_DEPTH + 0.1))
hex_recess = (hex_recess.union(reliefs)
              .rotate((0, 0, 0), (0, 0, 1), 30.0 - YAW)
              .translate((xL, 0, -0.1)))
body = body.cut(hex_recess)
# bolt holes and hex corners at 30 + 60k deg (world), pins at 60k deg
bolt_a0 = math.radians(30.0 - YAW)
bolts = [(xL + BOLT_CIRCLE_D / 2 * math.cos(bolt_a0 + 2 * math.pi * i / N_BOLT),
          BOLT_CIRCLE_D / 2 * math.sin(bolt_a0 + 2 * math.pi * i / N_BOLT))
         for i in range(N_BOLT)]
body = body.cut(cq.Workplane("XY").pushPoints(bolts).circle(BOLT_HOLE_D / 2)
                .extrude(zNut + 0.2).translate((0, 0, -0.1)))
pin_a0 = math.radians(0.0 - YAW)
pins = [(xL + PIN_CIRCLE_D / 2 * math.cos(pin_a0 + 2 * math.pi * i / 6),
         PIN_CIRCLE_D / 2 * math.sin(pin_a0 + 2 * math.pi * i / 6))
        for i in range(6)]
body = body.cut(cq.Workplane("XY").pushPoints(pins).circle(PIN_HOLE_D / 2)
                .extrude(SP_T + 0.2).translate((0, 0, -0.1)))

result = body.rotate((0, 0, 0), (0, 0, 1), YAW)

VIEW = {"azimuth": 45, "elevation": 26}
